import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 100.0          # overall length (Y)
W = 30.0           # overall width (X)
T_PAD = 4.0        # pad (base plate) top height
T_END = 3.35       # end strip: height of the end face
BUMP = 3.72        # end strip bead crest height
COVE_END = 3.4     # end bead ends here (distance from the end)
END_LEN = 4.0      # end strip length (each end)
R_PAD_EDGE = 1.0   # round on the free (-X) top edge of the pads

RIB_W = 7.5        # rib width (X), rib sits on +X edge
RIB_H = 14.5       # rib top height
RIB_R_OUT = 5.0    # big round on outer top edge
RIB_R_IN = 1.0     # small round on inner top edge
RIB_R_BASE = 1.0   # concave fillet rib / pad
RIB_Y0 = 4.0       # rib starts this far from each end

# J-shaped slot separating the pads (through whole width)
GAP_A = 30.9       # tongue tip (slot start) from -Y end
GAP_B = 37.05      # slot end
HOOK_Y = 27.4      # hook extends back to here
SLOT_TOP = 5.75    # slot top height
HOOK_LOW = 2.05    # hook lower edge (tongue top)
R_SLOT_TOP = 1.5
R_SLOT_BOT_A = 0.4  # tongue tip, bottom corner
R_SLOT_BOT_B = 0.9  # far wall, bottom corner
R_TONGUE = 0.7

# spring tabs (profile in XZ, extruded along Y)
TAB_W = 12.4
TAB_CENTERS = (13.4, 50.0, L - 13.4)
TAB_BASE_L = 12.42     # foot, -X side (at pad top)
TAB_KNEE_L = (13.45, 7.7)
TAB_TOP_L = (16.65, 10.9)
TAB_TOP_R = (20.3, 10.9)
TAB_KNEE_R = (17.15, 7.75)
TAB_BASE_R = 16.3      # foot, +X side (at pad top)
R_KNEE_OUT = 1.5
R_KNEE_IN = 1.0
R_TIP = 1.0
R_TAB_ROOT = 0.6

S45 = math.sqrt(0.5)


# ---------------- base plate (YZ profile, extruded along X) ----------------
def make_base():
    e = END_LEN
    cb = COVE_END
    prof = (cq.Workplane("YZ")
            .moveTo(0, 0)
            .lineTo(L, 0)
            .lineTo(L, T_END)
            .threePointArc((L - cb / 2.0, BUMP), (L - cb, T_END))
            .lineTo(L - e, T_PAD)
            .lineTo(e, T_PAD)
            .lineTo(cb, T_END)
            .threePointArc((cb / 2.0, BUMP), (0, T_END))
            .close()
            .extrude(W))
    # round the free -X top edge by intersecting with a rounded XZ section
    r = R_PAD_EDGE
    trim = (cq.Workplane("XZ", origin=(0, L + 1, 0))
            .moveTo(0, -1)
            .lineTo(W + 1, -1)
            .lineTo(W + 1, T_PAD + 1)
            .lineTo(r, T_PAD)
            .threePointArc((r - r * S45, T_PAD - r + r * S45), (0, T_PAD - r))
            .close()
            .extrude(L + 2))
    return prof.intersect(trim)


base = make_base()

# ---------------- rib (XZ profile, extruded along Y) ----------------
x0 = W - RIB_W
rb = RIB_R_BASE
rib = (cq.Workplane("XZ", origin=(0, L - RIB_Y0, 0))
       .moveTo(x0 - rb, 0)
       .lineTo(W, 0)
       .lineTo(W, RIB_H - RIB_R_OUT)
       .threePointArc((W - RIB_R_OUT + RIB_R_OUT * S45, RIB_H - RIB_R_OUT + RIB_R_OUT * S45),
                      (W - RIB_R_OUT, RIB_H))
       .lineTo(x0 + RIB_R_IN, RIB_H)
       .threePointArc((x0 + RIB_R_IN - RIB_R_IN * S45, RIB_H - RIB_R_IN + RIB_R_IN * S45),
                      (x0, RIB_H - RIB_R_IN))
       .lineTo(x0, T_PAD + rb)
       .threePointArc((x0 - rb + rb * S45, T_PAD + rb - rb * S45), (x0 - rb, T_PAD))
       .close()
       .extrude(L - 2 * RIB_Y0))

body = base.union(rib)


# ---------------- J slots ----------------
def j_cutter(mirror=False):
    a, b, hy = GAP_A, GAP_B, HOOK_Y
    rh = (SLOT_TOP - HOOK_LOW) / 2.0
    zc = (SLOT_TOP + HOOK_LOW) / 2.0
    rc, ra, rbt, rt = R_SLOT_TOP, R_SLOT_BOT_A, R_SLOT_BOT_B, R_TONGUE
    s = S45

    def P(y, z):
        return (L - y, z) if mirror else (y, z)

    wp = (cq.Workplane("YZ", origin=(-1, 0, 0))
          .moveTo(*P(a - ra, -1))
          .lineTo(*P(b + rbt, -1))
          .lineTo(*P(b + rbt, 0))
          .threePointArc(P(b + rbt - s * rbt, rbt - s * rbt), P(b, rbt))
          .lineTo(*P(b, SLOT_TOP - rc))
          .threePointArc(P(b - rc + s * rc, SLOT_TOP - rc + s * rc), P(b - rc, SLOT_TOP))
          .lineTo(*P(hy + rh, SLOT_TOP))
          .threePointArc(P(hy, zc), P(hy + rh, HOOK_LOW))
          .lineTo(*P(a - rt, HOOK_LOW))
          .threePointArc(P(a - rt + s * rt, HOOK_LOW - rt + s * rt), P(a, HOOK_LOW - rt))
          .lineTo(*P(a, ra))
          .threePointArc(P(a - ra + s * ra, ra - s * ra), P(a - ra, 0))
          .close())
    return wp.extrude(W + 2)


body = body.cut(j_cutter(False)).cut(j_cutter(True))


# ---------------- spring tabs ----------------
def edge_filter(pred):
    class _Sel(cq.Selector):
        def filter(self, objs):
            return [o for o in objs if pred(o)]
    return _Sel()


def near(v, p, tol=0.05):
    return abs(v.x - p[0]) < tol and abs(v.z - p[1]) < tol


def make_tab(yc):
    # extend the lower legs below the pad top so the tab merges with the pad
    zb = T_PAD - 1.0
    kx, kz = TAB_KNEE_L
    sl = (kx - TAB_BASE_L) / (kz - T_PAD)
    kx2, kz2 = TAB_KNEE_R
    sr = (kx2 - TAB_BASE_R) / (kz2 - T_PAD)
    xl0 = TAB_BASE_L - sl * (T_PAD - zb)
    xr0 = TAB_BASE_R - sr * (T_PAD - zb)
    pts = [(xl0, zb), TAB_KNEE_L, TAB_TOP_L, TAB_TOP_R, TAB_KNEE_R, (xr0, zb)]
    tab = (cq.Workplane("XZ", origin=(0, yc + TAB_W / 2.0, 0))
           .polyline(pts).close()
           .extrude(TAB_W))
    # knees
    tab = tab.edges(edge_filter(lambda e: near(e.Center(), TAB_KNEE_L) and
                                abs(e.Center().y - yc) < 0.1)).fillet(R_KNEE_OUT)
    tab = tab.edges(edge_filter(lambda e: near(e.Center(), TAB_KNEE_R) and
                                abs(e.Center().y - yc) < 0.1)).fillet(R_KNEE_IN)

    # round the outer (+X side) profile edges of both side faces
    def mid_x(z):
        ml = [(zb, (xl0 + xr0) / 2.0),
              (TAB_KNEE_L[1], (TAB_KNEE_L[0] + TAB_KNEE_R[0]) / 2.0),
              (TAB_TOP_L[1], (TAB_TOP_L[0] + TAB_TOP_R[0]) / 2.0)]
        for (z0, x0_), (z1, x1_) in zip(ml[:-1], ml[1:]):
            if z <= z1:
                t = (z - z0) / (z1 - z0)
                return x0_ + t * (x1_ - x0_)
        return ml[-1][1]

    def outer_side_edge(e):
        c = e.Center()
        if abs(abs(c.y - yc) - TAB_W / 2.0) > 0.05:
            return False
        if c.z > TAB_TOP_L[1] - 0.05 or c.z < zb + 0.05:
            return False
        return c.x > mid_x(c.z)

    tab = tab.edges(edge_filter(outer_side_edge)).fillet(R_TIP)
    return tab


for yc in TAB_CENTERS:
    body = body.union(make_tab(yc))


# fillet the tab roots on the pad
def root_edge(e):
    c = e.Center()
    bb = e.BoundingBox()
    if bb.zmax - bb.zmin > 0.02 or abs(c.z - T_PAD) > 0.02:
        return False
    if not (TAB_BASE_L - 0.5 < c.x < TAB_KNEE_R[0] + 0.5):
        return False
    return any(abs(c.y - yc) < TAB_W / 2.0 + 0.3 for yc in TAB_CENTERS)


body = body.edges(edge_filter(root_edge)).fillet(R_TAB_ROOT)

result = body.translate((-W / 2.0, -L / 2.0, 0))
